import math
import cadquery as cq
from OCP.Geom import Geom_BSplineCurve
from OCP.TColgp import TColgp_Array1OfPnt
from OCP.TColStd import TColStd_Array1OfReal, TColStd_Array1OfInteger
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge, BRepBuilderAPI_MakeWire
from OCP.gp import gp_Pnt, gp_Dir, gp_Ax2, gp_Circ

# ------------------------------------------------------------------
# Bent round rod ("twisted hairpin"): a solid rod of diameter D bent
# into a tight U at the apex, the two legs opening into a V (top view)
# while one leg climbs and the other descends (side view).
# The part is symmetric under a 180 deg rotation about the Y axis:
#      (x, y, z) -> (-x, y, -z)
# ------------------------------------------------------------------

D = 10.0                        # rod diameter (mm)

# Centre-line of the right half (apex -> right free end), as cubic
# B-spline control points in units of D.  Apex at the origin, apex tangent
# along +X, legs running toward +Y.
APEX_HANDLE = 0.1984                     # apex tangent handle length
MID_CTRL = [(0.5681, 0.2004, 0.0761),    # interior control points
            (0.6293, 0.9891, 0.0430)]
END_PT = (1.5209, 4.5816, 1.3776)        # centre of the right end face
END_DIR = (0.1503, 1.0, 0.4117)          # leg direction at the end face
END_HANDLE = 2.2752                       # end tangent handle length
SEAM_ANGLE = 320.0                       # where the sweep seam starts (deg)

VIEW = {"azimuth": 45, "elevation": 26}


def unit(v):
    n = math.sqrt(sum(c * c for c in v))
    return tuple(c / n for c in v)


def rot(p):
    """Part symmetry: 180 deg rotation about the Y axis."""
    return (-p[0], p[1], -p[2])


# ---- right-half control polygon ----
T_end = unit(END_DIR)
right = [(APEX_HANDLE, 0.0, 0.0)] + [tuple(p) for p in MID_CTRL] + [
    tuple(END_PT[i] - END_HANDLE * T_end[i] for i in range(3)),
    tuple(END_PT),
]
n_half = len(right) + 1                  # poles per half (incl. the apex)

# ---- one C1 B-spline for the whole rod: left half + right half ----
# each half is a clamped uniform cubic B-spline (apex, right..., end);
# the two halves meet at the apex with collinear, equal handles (G1/C1).
poles = [rot(p) for p in reversed(right)] + [(0.0, 0.0, 0.0)] + right
n_int = n_half - 4                       # interior knots per half
half_knots = [(i + 1) / (n_int + 1) for i in range(n_int)]
knots = [-1.0] + [-k for k in reversed(half_knots)] + [0.0] + half_knots + [1.0]
mults = [4] + [1] * n_int + [3] + [1] * n_int + [4]

arr = TColgp_Array1OfPnt(1, len(poles))
for i, p in enumerate(poles):
    arr.SetValue(i + 1, gp_Pnt(p[0] * D, p[1] * D, p[2] * D))
k_arr = TColStd_Array1OfReal(1, len(knots))
m_arr = TColStd_Array1OfInteger(1, len(knots))
for i, (k, m) in enumerate(zip(knots, mults)):
    k_arr.SetValue(i + 1, k)
    m_arr.SetValue(i + 1, m)
centre_line = Geom_BSplineCurve(arr, k_arr, m_arr, 3)
# the apex joint is C1 (collinear, equal handles): drop the extra knot
_i0 = [i for i in range(1, centre_line.NbKnots() + 1)
       if abs(centre_line.Knot(i)) < 1e-12][0]
centre_line.RemoveKnot(_i0, 2, 1e-7)
path = cq.Wire(
    BRepBuilderAPI_MakeWire(BRepBuilderAPI_MakeEdge(centre_line).Edge()).Wire()
)

# ---- circular cross-section at the left free end ----
start = rot(END_PT)
start_dir = unit(rot(T_end))
start_dir = (-start_dir[0], -start_dir[1], -start_dir[2])   # into the rod
# seam reference direction: perpendicular to the path tangent
ref = (0.0, 0.0, 1.0)
cx = (ref[1] * start_dir[2] - ref[2] * start_dir[1],
      ref[2] * start_dir[0] - ref[0] * start_dir[2],
      ref[0] * start_dir[1] - ref[1] * start_dir[0])
cx = unit(cx)
cy = (start_dir[1] * cx[2] - start_dir[2] * cx[1],
      start_dir[2] * cx[0] - start_dir[0] * cx[2],
      start_dir[0] * cx[1] - start_dir[1] * cx[0])
sa = math.radians(SEAM_ANGLE)
xdir = tuple(math.cos(sa) * cx[i] + math.sin(sa) * cy[i] for i in range(3))
ax = gp_Ax2(gp_Pnt(*[c * D for c in start]), gp_Dir(*start_dir), gp_Dir(*xdir))
circle = BRepBuilderAPI_MakeEdge(gp_Circ(ax, D / 2.0)).Edge()
profile = cq.Wire(BRepBuilderAPI_MakeWire(circle).Wire())

rod = cq.Solid.sweep(profile, [], path, makeSolid=True, isFrenet=False)

result = cq.Workplane("XY").add(rod)
